import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 118.0          # overall width (X)
FRAME_D = 86.0     # depth of rectangular frame part (Y)
BACK_Y = 65.0      # back edge of tab band (Y)
CH_X = 33.0        # half-length of back edge (chamfer start)
T = 1.3            # plate thickness

PAD_X = 19.5       # corner pad width (X)
PAD_Y_F = 14.8     # front corner pad depth (Y)
PAD_Y_B = 15.2     # back corner pad depth (Y, below the chamfer end)
STRIP_IN = 3.2     # side strip inset from outer edge
STRIP_W = 6.2      # side strip width
FSTRIP_OFF = 2.45  # front thin strip offset from front edge
FSTRIP_W = 0.9    # front thin strip width

WIN_TOP = 39.4     # window top edge (Y)
NOTCH_TOP = 41.5   # middle notch top edge (Y)
NOTCH_HX = 18.7    # half width of middle notch

POST = 9.1         # post square size
R_OO = 3.8         # post corner radius at the outer (frame-corner) corner
R_II = 4.1         # post corner radius at the inner (frame-centre) corner
R_OFF = 1.1        # post corner radius at the two off-diagonal corners
POST_EPS = 0.03    # tiny inset of the post from the pad edges (robust booleans)
BACK_POST_IN = 0.45  # back posts sit slightly in front of the chamfer end
TALL_H = 23.25     # tall (back) post height from bottom
SHORT_H = 9.5      # short (front) post height from bottom
PIN_D = 2.7        # blind cross hole diameter in posts
PIN_DEPTH = 4.0
TALL_PIN_Z = 15.5
SHORT_PIN_Z = 6.2

HOLE_SIDE_D = 12.5
HOLE_SIDE_X = 32.8
HOLE_SIDE_Y = 51.1
HOLE_MID_D = 15.5
HOLE_MID_Y = 53.5
KEY_X = 18.0
KEY_Y = 58.2
KEY_D = 6.3
KEY_SLOT_W = 2.2
KEY_SLOT_END = 48.7

hw = W / 2.0
fy = -FRAME_D / 2.0      # front edge
by = FRAME_D / 2.0       # back pad top (chamfer end)
pad_in_x = hw - PAD_X
bpad_bot = by - PAD_Y_B
fpad_top = fy + PAD_Y_F

# ---------------- plate ----------------
back_pts = [
    (-hw, bpad_bot), (-hw, by), (-CH_X, BACK_Y), (CH_X, BACK_Y), (hw, by),
    (hw, bpad_bot), (pad_in_x, bpad_bot), (pad_in_x, WIN_TOP),
    (NOTCH_HX, WIN_TOP), (NOTCH_HX, NOTCH_TOP), (-NOTCH_HX, NOTCH_TOP),
    (-NOTCH_HX, WIN_TOP), (-pad_in_x, WIN_TOP), (-pad_in_x, bpad_bot),
]
plate = cq.Workplane("XY").polyline(back_pts).close().extrude(T)

for sx in (-1, 1):
    # side strips (inset from the outer edge)
    cx = sx * (hw - STRIP_IN - STRIP_W / 2.0)
    strip = (cq.Workplane("XY")
             .center(cx, (bpad_bot + fpad_top) / 2.0)
             .rect(STRIP_W, bpad_bot - fpad_top + 2.0).extrude(T))
    plate = plate.union(strip)
    # front corner pads
    pad = (cq.Workplane("XY")
           .center(sx * (hw - PAD_X / 2.0), fy + PAD_Y_F / 2.0)
           .rect(PAD_X, PAD_Y_F).extrude(T))
    plate = plate.union(pad)

# thin front tie strip between the front pads
fstrip = (cq.Workplane("XY")
          .center(0, fy + FSTRIP_OFF + FSTRIP_W / 2.0)
          .rect(2 * pad_in_x + 1.0, FSTRIP_W).extrude(T))
plate = plate.union(fstrip)

# ---------------- holes in back band ----------------
holes = (cq.Workplane("XY")
         .pushPoints([(-HOLE_SIDE_X, HOLE_SIDE_Y), (HOLE_SIDE_X, HOLE_SIDE_Y)])
         .circle(HOLE_SIDE_D / 2.0).extrude(T)
         .union(cq.Workplane("XY").center(0, HOLE_MID_Y)
                .circle(HOLE_MID_D / 2.0).extrude(T)))
for sx in (-1, 1):
    kc = cq.Workplane("XY").center(sx * KEY_X, KEY_Y).circle(KEY_D / 2.0).extrude(T)
    ks = (cq.Workplane("XY").center(sx * KEY_X, (KEY_Y + KEY_SLOT_END) / 2.0)
          .rect(KEY_SLOT_W, KEY_Y - KEY_SLOT_END).extrude(T))
    holes = holes.union(kc).union(ks)
plate = plate.cut(holes)


# ---------------- posts ----------------
def post_section_pts(start_corner):
    """Through-points of the post section in a local frame where +x/+y point
    outwards (towards the frame corner).  Rounded square with a different
    radius on each corner; the list starts at the middle of the arc of
    `start_corner` (index 0..3 = (+,+), (-,+), (-,-), (+,-))."""
    h = POST / 2.0
    radii = [R_OO, R_OFF, R_II, R_OFF]
    signs = [(1, 1), (-1, 1), (-1, -1), (1, -1)]
    arcs = []
    for i in range(4):
        r = radii[i]
        ux, uy = signs[i]
        ccx, ccy = ux * (h - r), uy * (h - r)
        a0 = math.pi / 2.0 * i
        arcs.append([(ccx + r * math.cos(a0 + d), ccy + r * math.sin(a0 + d))
                     for d in (0.0, math.pi / 4.0, math.pi / 2.0)])
    pts = []
    for j in range(4):
        i = (start_corner + j) % 4
        nxt = arcs[(i + 1) % 4]
        arc = arcs[i]
        side_mid = ((arc[2][0] + nxt[0][0]) / 2.0, (arc[2][1] + nxt[0][1]) / 2.0)
        pts += [arc[1], arc[2], side_mid, nxt[0]]
    return pts


def post(sx, sy, y_edge, h):
    """Post standing in the corner (sx, sy) whose outer faces sit on the
    pad edges x = sx*hw and y = y_edge."""
    # seam at the world (+X,+Y) corner of every post
    start = {(1, 1): 0, (-1, 1): 1, (-1, -1): 2, (1, -1): 3}[(sx, sy)]
    local = post_section_pts(start)
    edge = cq.Edge.makeSpline([cq.Vector(x, y, 0) for x, y in local], periodic=True)
    samples = [edge.positionAt(i / 720.0) for i in range(720)]
    mx = max(p.x for p in samples)
    my = max(p.y for p in samples)
    ox = sx * (hw - POST_EPS - mx)
    oy = y_edge - sy * (POST_EPS + my)
    pts = [(ox + sx * x, oy + sy * y) for x, y in local]
    z0 = T * 0.5
    return (cq.Workplane("XY").workplane(offset=z0)
            .spline(pts, periodic=True).close().extrude(h - z0))


result = plate
pcx = hw - POST / 2.0
for sx in (-1, 1):
    # tall back posts, blind pin hole in the +Y (back) face
    tp = post(sx, 1, by - BACK_POST_IN, TALL_H)
    pin = (cq.Workplane("XZ", origin=(0, by - BACK_POST_IN + 0.5, 0))
           .center(sx * pcx, TALL_PIN_Z).circle(PIN_D / 2.0).extrude(PIN_DEPTH + 0.5))
    result = result.union(tp).cut(pin)
    # short front posts, blind pin hole in the -Y (front) face
    sp = post(sx, -1, fy, SHORT_H)
    pin2 = (cq.Workplane("XZ", origin=(0, fy - 0.5, 0))
            .center(sx * pcx, SHORT_PIN_Z).circle(PIN_D / 2.0).extrude(-PIN_DEPTH - 0.5))
    result = result.union(sp).cut(pin2)

VIEW = {"azimuth": 45, "elevation": 26}
